import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 90.0          # outer width (X) and depth (Y) - square footprint
H = 22.0          # overall height
R_V = 10.0        # vertical corner radius (plan view)
R_T = 9.5         # top edge fillet radius
T = 1.6           # wall / ceiling thickness

# corner screw posts
POST_OFF = 37.3   # hole centre offset from part centre (X and Y)
POST_IN = 34.4    # inner face of corner post (from centre)
POST_H = 8.0      # post height from rim
POST_R = 2.9      # rounding of the post's inner vertical edge
POST_HOLE_D = 2.5
POST_HOLE_DEPTH = 7.0

# side slots (obround through the wall)
SLOT_Z = 15.45
SLOT_H = 2.2
SLOT_XP_L = 15.0  # +X wall slot length (along Y), centred
SLOT_XN_L = 10.5  # -X wall slot length (along Y)
SLOT_XN_Y = 26.8

# vent slots in the top
VENT_X = -23.6
VENT_Y = 0.0
VENT_N = 3
VENT_W = 0.85
VENT_L = 7.2
VENT_PITCH = 1.6

# internal PCB standoffs
BOSS_X = -23.2
BOSS_Y = (-14.5, 13.1)
BOSS_D = 4.4
BOSS_H = 4.1
BOSS_HOLE_D = 2.2

# internal rib next to the upper standoff
RIB_X0, RIB_X1 = -35.6, -22.6
RIB_Y = 18.2
RIB_T = 2.0
RIB_H = 5.15

# internal U-channel
CH_X0, CH_X1 = -35.6, -22.6
CH_Y = 34.8
CH_W = 3.0        # overall width of the channel (Y)
CH_GAP = 1.0      # groove width
CH_H = 5.2
CH_COMB_N = 5     # small pockets in the channel's front face
CH_COMB_PITCH = 2.54
CH_COMB_W = 1.9
CH_COMB_H = 0.6
CH_COMB_D = 0.6
CH_COMB_DZ = 2.0   # pocket row centre below the ceiling

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- outer body ----------------
outer = (
    cq.Workplane("XY")
    .box(W, W, H, centered=(True, True, False))
    .edges("|Z").fillet(R_V)
    .edges(">Z").fillet(R_T)
)

body = outer.faces("<Z").shell(-T)

ceil_z = H - T

# ---------------- corner screw posts ----------------
post_size = W / 2 - POST_IN
posts = None
for sx in (-1, 1):
    for sy in (-1, 1):
        cx = sx * (POST_IN + post_size / 2)
        cy = sy * (POST_IN + post_size / 2)
        p = (
            cq.Workplane("XY")
            .center(cx, cy)
            .box(post_size, post_size, POST_H, centered=(True, True, False))
            .edges("|Z")
            .edges(cq.selectors.NearestToPointSelector((sx * POST_IN, sy * POST_IN, POST_H / 2)))
            .fillet(POST_R)
        )
        posts = p if posts is None else posts.union(p)
posts = posts.intersect(outer)
body = body.union(posts)

# holes in posts
for sx in (-1, 1):
    for sy in (-1, 1):
        h = (
            cq.Workplane("XY")
            .workplane(offset=-0.1)
            .center(sx * POST_OFF, sy * POST_OFF)
            .circle(POST_HOLE_D / 2)
            .extrude(POST_HOLE_DEPTH + 0.1)
        )
        body = body.cut(h)

# ---------------- internal standoffs ----------------
for by in BOSS_Y:
    boss = (
        cq.Workplane("XY")
        .workplane(offset=ceil_z - BOSS_H)
        .center(BOSS_X, by)
        .circle(BOSS_D / 2)
        .extrude(BOSS_H + 0.5)
    )
    body = body.union(boss)
    hole = (
        cq.Workplane("XY")
        .workplane(offset=ceil_z - BOSS_H - 0.1)
        .center(BOSS_X, by)
        .circle(BOSS_HOLE_D / 2)
        .extrude(BOSS_H)
    )
    body = body.cut(hole)

# ---------------- internal rib ----------------
rib = (
    cq.Workplane("XY")
    .workplane(offset=ceil_z - RIB_H)
    .center((RIB_X0 + RIB_X1) / 2, RIB_Y + RIB_T / 2)
    .rect(RIB_X1 - RIB_X0, RIB_T)
    .extrude(RIB_H + 0.5)
)
body = body.union(rib)

# ---------------- internal U-channel ----------------
ch = (
    cq.Workplane("XY")
    .workplane(offset=ceil_z - CH_H)
    .center((CH_X0 + CH_X1) / 2, CH_Y)
    .rect(CH_X1 - CH_X0, CH_W)
    .extrude(CH_H + 0.5)
)
ch_groove = (
    cq.Workplane("XY")
    .workplane(offset=ceil_z - CH_H - 0.1)
    .center((CH_X0 + CH_X1) / 2, CH_Y)
    .rect(CH_X1 - CH_X0 + 1, CH_GAP)
    .extrude(CH_H - 1.0)
)
# row of small pockets in the channel's front face (header-pitch comb)
ch_front_y = CH_Y - CH_W / 2
comb_pts = [
    ((CH_X0 + CH_X1) / 2 + (i - (CH_COMB_N - 1) / 2) * CH_COMB_PITCH, ceil_z - CH_COMB_DZ)
    for i in range(CH_COMB_N)
]
ch_comb = (
    cq.Workplane("XZ", origin=(0, ch_front_y - 0.1, 0))
    .pushPoints(comb_pts)
    .rect(CH_COMB_W, CH_COMB_H)
    .extrude(-CH_COMB_D - 0.1)
)
body = body.union(ch.cut(ch_groove).cut(ch_comb))

# ---------------- side slots ----------------
slot_xp = (
    cq.Workplane("YZ")
    .workplane(offset=W / 2 - T - 1)
    .center(0, SLOT_Z)
    .slot2D(SLOT_XP_L, SLOT_H, 0)
    .extrude(T + 3)
)
body = body.cut(slot_xp)

slot_xn = (
    cq.Workplane("YZ")
    .workplane(offset=-W / 2 - 1)
    .center(SLOT_XN_Y, SLOT_Z)
    .slot2D(SLOT_XN_L, SLOT_H, 0)
    .extrude(T + 3)
)
body = body.cut(slot_xn)

# ---------------- top vents ----------------
vent_pts = [
    (VENT_X + (i - (VENT_N - 1) / 2) * VENT_PITCH, VENT_Y) for i in range(VENT_N)
]
vents = (
    cq.Workplane("XY")
    .workplane(offset=ceil_z - 1)
    .pushPoints(vent_pts)
    .slot2D(VENT_L, VENT_W, 90)
    .extrude(T + 3)
)
body = body.cut(vents)

result = body
